import cadquery as cq
import math

# ================= driving dimensions (mm) =================
W = 60.0      # X extent
D = 50.7      # Y extent
H = 60.0      # Z extent
T = 5.25      # thickness of the central angle legs
TW = 5.3      # back wall thickness (Y)
TG = 5.3      # gusset plate thickness
XL = 34.8     # vertical leg inner face (X)
XR = XL + T   # vertical leg outer face (X)
ZB = 19.95    # horizontal leg underside (Z)
ZT = ZB + T   # horizontal leg top (Z)
YW = D - TW   # inner face of back walls (Y)
CH = 3.7      # 45 deg root chamfer size
ACH = 4.0     # outer chamfer on the angle corner
R_BIG = 6.7   # pivot bore radius
FLAT = 6.45   # pivot bore flat distance
R_CB = 8.5    # pivot counterbore radius
CBD = 6.0     # pivot counterbore depth
WF = 3.5      # fillet at upper wall / horizontal leg junction
R_SM = 2.15   # small screw hole radius
R_HC = 3.8    # screw head clearance radius
BOSS_R = 11.2 # pivot boss radius
BOSS_T = 9.0  # pivot boss thickness (from outer face)
CLR1 = 12.6   # swing clearance radius (outer zone)
CLR2 = 9.5    # swing clearance radius (inner zone)
PKD = 3.8     # pocket depth
PKR = 0.8     # pocket corner radius (at floor)
PK_DRAFT = 21.5  # pocket wall draft angle (deg)

# upper pivot (axis along X)
UY, UZ = 11.2, 32.8
# lower pivot (axis along Z)
LX, LY = 27.3, 37.8
# swing-clearance zone split (upper: along X, lower: along Z = W - X)
X_MID = 44.0
SLOT_HW = 5.95            # half width of the rear exit slot of the lower clearance
# screw holes
UW_HOLE = (50.0, 50.0)    # upper back wall hole (X, Z), axis Y
UL_HOLE = (50.0, 34.5)    # horizontal leg hole (X, Y), axis Z
LW_HOLE = (10.0, 10.0)    # lower back wall hole (X, Z), axis Y
LL_HOLE = (10.0, 10.0)    # vertical leg hole (Y, Z), axis X
SLANT_TOP_Y = 45.1        # where the gusset slanted edge meets the top (Y)


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def dprofile(r, flat):
    """Pivot bore profile: circle with a flat (and 45 deg corners) on local -y side."""
    h = flat * math.tan(math.radians(22.5)) * 1.12
    a = flat + h
    # intersection of 45 deg line x+|y| = a with circle r  (local frame: flat normal = +x)
    t = (a - math.sqrt(2 * r * r - a * a)) / 2.0
    p = (a - t, t)
    return (flat, h), p


def bore(plane, origin, cx, cy, r, flat, length, flat_dir):
    """D-shaped bore; flat_dir is the 2D direction (local) of the flat."""
    (fx, fh), p = dprofile(r, flat)
    ux, uy = flat_dir
    vx, vy = -uy, ux

    def loc(a, b):
        return (cx + a * ux + b * vx, cy + a * uy + b * vy)

    wp = cq.Workplane(plane, origin=origin)
    s = (wp.moveTo(*loc(fx, -fh)).lineTo(*loc(fx, fh)).lineTo(*loc(p[0], p[1]))
         .threePointArc(loc(-r, 0), loc(p[0], -p[1])).close())
    return s.extrude(length)


# ================= central angle (L profile along Y) =================
angle = (cq.Workplane("XZ")
         .polyline([(XL, 0), (XR, 0), (XR, ZB), (W, ZB), (W, ZT), (XL + ACH, ZT), (XL, ZT - ACH)])
         .close().extrude(-D))

# ================= back walls =================
# web between the two back walls (continues the angle's corner chamfer plane)
CHL = XL + ACH - ZT          # chamfer plane: X - Z = CHL
YWEB = 42.6
web = (cq.Workplane("XZ", origin=(0, YWEB, 0))
       .polyline([(CHL + ZB, ZB), (XR, ZB), (XR, XR - CHL)]).close().extrude(-(D - YWEB)))
upper_wall = box(XR, W, YW, D, ZB, H)
lower_wall = box(0, XR, YW, D, 0, ZB)

# ================= upper gusset (YZ plane, at X max) =================
P = (SLANT_TOP_Y, H)
dx, dy = P[0] - UY, P[1] - UZ
ang = math.atan2(dy, dx) + math.acos(BOSS_R / math.hypot(dx, dy))
tp = (UY + BOSS_R * math.cos(ang), UZ + BOSS_R * math.sin(ang))
mid_ang = (ang + math.pi) / 2
mp = (UY + BOSS_R * math.cos(mid_ang), UZ + BOSS_R * math.sin(mid_ang))


def upper_profile(x0, x1):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .moveTo(0, ZB).lineTo(D, ZB).lineTo(D, H).lineTo(P[0], H)
            .lineTo(*tp).threePointArc(mp, (0, UZ)).close()
            .extrude(x1 - x0))


ug = upper_profile(W - TG, W)
uclip = upper_profile(XR, W)
# pivot boss with 45 deg blend cone into the gusset
ub_x0 = W - BOSS_T
BF = W - TG - ub_x0   # 45 deg blend (boss -> gusset face)
uboss = (cq.Workplane("XY", origin=(0, UY, UZ))
         .moveTo(ub_x0, 0).lineTo(ub_x0, BOSS_R).lineTo(ub_x0 + BF, BOSS_R + BF)
         .lineTo(W, BOSS_R + BF).lineTo(W, 0).close()
         .revolve(360, (0, 0, 0), (1, 0, 0))
         .union(box(ub_x0, W, 0, UY, ZB, UZ))
         .intersect(uclip))
# root chamfers
uch_leg = (cq.Workplane("XZ").polyline([(W - TG, ZT), (W - TG - CH, ZT), (W - TG, ZT + CH)]).close()
           .extrude(-D))
uch_wall = (cq.Workplane("XY").polyline([(W - TG, YW), (W - TG - CH, YW), (W - TG, YW - CH)]).close()
            .extrude(H))
uch = uch_leg.union(uch_wall).intersect(uclip)

# ================= lower gusset (XY plane, at Z min) =================
tri_pts = [(0, YW), (XL, YW), (XL, 0)]
lclip = (cq.Workplane("XY").polyline(tri_pts).close().extrude(H)
         .union(box(0, XR, YW - 1, D, 0, H)).union(box(XL - 1, XR, 0, D, 0, H)))
lg = cq.Workplane("XY").polyline(tri_pts).close().extrude(TG)
lch_wall = (cq.Workplane("YZ").polyline([(YW, TG), (YW - CH, TG), (YW, TG + CH)]).close().extrude(XR))
lch_leg = (cq.Workplane("XZ").polyline([(XL, TG), (XL - CH, TG), (XL, TG + CH)]).close().extrude(-D))
lclip_ch = cq.Workplane("XY").polyline(tri_pts).close().extrude(H)
lch = lch_wall.union(lch_leg).intersect(lclip_ch)
LB_X0, LB_Y0 = 16.4, 26.3   # lower boss top face: -X and -Y side positions
LB_RC = 10.0                 # lower boss top face corner radius
LB_BL = 3.0                  # lower boss blend width (over height BOSS_T - TG)
lb_taper = math.degrees(math.atan(LB_BL / (BOSS_T - TG)))
lb_sk = (cq.Sketch().push([(LB_X0 - LB_BL + 20.0, LB_Y0 - LB_BL + 20.0)])
         .rect(40.0, 40.0).reset().vertices().fillet(LB_RC + LB_BL))
lboss = (cq.Workplane("XY", origin=(0, 0, TG)).placeSketch(lb_sk)
         .extrude(BOSS_T - TG, taper=lb_taper)
         .intersect(lclip))

# concave fillet at the base of the upper wall (wall face / horizontal leg top)
uwf = (cq.Workplane("YZ", origin=(XR, 0, 0))
       .moveTo(YW, ZT).lineTo(YW - WF, ZT)
       .threePointArc((YW - WF * (1 - math.sqrt(0.5)), ZT + WF * (1 - math.sqrt(0.5))), (YW, ZT + WF))
       .close().extrude(W - TG - CH - XR))

body = (angle.union(web).union(upper_wall).union(uwf).union(lower_wall)
        .union(ug).union(uboss).union(uch)
        .union(lg).union(lch).union(lboss))

# ================= swing clearance cuts =================
ucl = (cq.Workplane("YZ", origin=(XL - 0.2, 0, 0)).center(UY, UZ).circle(CLR1).extrude(X_MID - XL + 0.2)
       .union(cq.Workplane("YZ", origin=(X_MID, 0, 0)).center(UY, UZ).circle(CLR2).extrude(ub_x0 - X_MID)))
body = body.cut(ucl)
z_mid = W - X_MID
lcl = (cq.Workplane("XY", origin=(0, 0, z_mid)).center(LX, LY).circle(CLR1).extrude(H)
       .union(cq.Workplane("XY", origin=(0, 0, BOSS_T)).center(LX, LY).circle(CLR2).extrude(z_mid - BOSS_T))
       .union(box(LX - SLOT_HW, LX + SLOT_HW, LY, D + 1, z_mid, H)))
body = body.cut(lcl)

# ================= lightening pockets =================
PK_R_ARC = 11.0   # pocket relief radius around the pivot bore


def arc_pt(cx, cy, r, a):
    return (cx + r * math.cos(a), cy + r * math.sin(a))


# upper gusset pocket (outer face X = W), floor profile in (Y, Z)
UPK_R = 11.0                     # floor relief radius around the bore
uz0, uy1 = 25.7, 46.45           # floor bottom edge (Z), floor +Y edge (Y)
tl = (16.68, 41.03)              # point on floor top edge
uslope = 0.432                   # floor top edge slope
tr = (uy1, tl[1] + uslope * (uy1 - tl[0]))
ua0 = -math.acos((UZ - uz0) / UPK_R)          # bottom line / arc
yb = UY + UPK_R * math.cos(ua0)
dvx, dvy = tl[0] - tr[0], tl[1] - tr[1]
dl = math.hypot(dvx, dvy); dvx, dvy = dvx / dl, dvy / dl
ox, oy = tr[0] - UY, tr[1] - UZ
bq = ox * dvx + oy * dvy
sq = -bq - math.sqrt(bq * bq - (ox * ox + oy * oy - UPK_R ** 2))
ptl = (tr[0] + sq * dvx, tr[1] + sq * dvy)
ua1 = math.atan2(ptl[1] - UZ, ptl[0] - UY)
uam = arc_pt(UY, UZ, UPK_R, (ua0 + ua1) / 2)
upk_sk = (cq.Sketch().segment((yb, uz0), (uy1, uz0)).segment(tr).segment(ptl)
          .arc(uam, (yb, uz0)).assemble().vertices().fillet(PKR))
upk = (cq.Workplane(cq.Plane(origin=(W - PKD, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0)))
       .placeSketch(upk_sk).extrude(PKD + 1, taper=-PK_DRAFT))
body = body.cut(upk)

# lower gusset pocket (outer face Z = 0), profile in (X, Y)
ly1, lx1, lyA, lxB = 46.5, 35.2, 5.52, 3.7
la0 = math.pi - math.asin((ly1 - LY) / PK_R_ARC)
lxa = LX + PK_R_ARC * math.cos(la0)
la1 = -math.acos((lx1 - LX) / PK_R_ARC) + 2 * math.pi
lya = LY + PK_R_ARC * math.sin(la1)
lam = arc_pt(LX, LY, PK_R_ARC, (la0 + la1) / 2)
# plane with normal -Z: local (x, y) = (X, -Y)
lpk_sk = (cq.Sketch().segment((lxB, -ly1), (lxa, -ly1)).arc((lam[0], -lam[1]), (lx1, -lya))
          .segment((lx1, -lyA)).close().assemble().vertices().fillet(PKR))
lpk = (cq.Workplane(cq.Plane(origin=(0, 0, PKD), xDir=(1, 0, 0), normal=(0, 0, -1)))
       .placeSketch(lpk_sk).extrude(PKD + 1, taper=-PK_DRAFT))
body = body.cut(lpk)

# ================= pivot bores =================
ubore = bore("YZ", (-1, 0, 0), UY, UZ, R_BIG, FLAT, W + 2, (-1, 0))
ucb = bore("YZ", (ub_x0 - 1, 0, 0), UY, UZ, R_CB, R_CB * 0.963, CBD + 1, (-1, 0))
lbore = bore("XY", (0, 0, -1), LX, LY, R_BIG, FLAT, H + 2, (0, -1))
lcb = bore("XY", (0, 0, BOSS_T - CBD), LX, LY, R_CB, R_CB * 0.963, CBD + 1, (0, -1))
body = body.cut(ubore).cut(ucb).cut(lbore).cut(lcb)

# ================= screw holes with head clearance =================
def yhole(x, z):
    return (cq.Workplane("XZ", origin=(0, D + 1, 0)).center(x, z).circle(R_SM).extrude(TW + 2)
            .union(cq.Workplane("XZ", origin=(0, YW, 0)).center(x, z).circle(R_HC).extrude(6)))


uwh = yhole(*UW_HOLE)
ulh = (cq.Workplane("XY", origin=(0, 0, ZB - 1)).center(*UL_HOLE).circle(R_SM).extrude(T + 2)
       .union(cq.Workplane("XY", origin=(0, 0, ZT)).center(*UL_HOLE).circle(R_HC).extrude(6)))
lwh = yhole(*LW_HOLE)
llh = (cq.Workplane("YZ", origin=(XL - 1, 0, 0)).center(*LL_HOLE).circle(R_SM).extrude(T + 2)
       .union(cq.Workplane("YZ", origin=(XL - 6, 0, 0)).center(*LL_HOLE).circle(R_HC).extrude(6)))
body = body.cut(uwh).cut(ulh).cut(lwh).cut(llh)

# ================= square vent windows into the clearances =================
win1 = box(XR + 0.01, 43.7, 11.5, 15.3, ZB - 1, ZB + 2)
win2 = box(XR - 2, XR + 1, 38.0, 41.8, 16.2, ZB)
body = body.cut(win1).cut(win2)

# ================= small catch tabs =================
tab_b = box(XR - 0.5, XR + 3.3, 13.9, 18.8, 8.2, 10.7).edges("|Y and >X and >Z").chamfer(1.35)
tab_a = box(49.3, 52.05, 37.8, 42.3, ZB - 3.3, ZB + 0.5).edges("|Y and <X and <Z").chamfer(1.3)
body = body.union(tab_b).union(tab_a)

result = body
